import math
import cadquery as cq

# =====================================================================
#  Shroud / cover with a vented box on top and a clevis tab
#  X across, Y along the tunnel (flared back end at +Y), Z up, bottom at z = 0
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
T = 4.0                 # wall thickness of the shroud
Y_BACK = 70.0           # back (flared) end of the shell

# outer arch sections along Y:
#   (y, x-centre, half-width a, crown height b, exponent right side, exponent left side)
# each half of a section is a superellipse |x/a|^n + |z/b|^n = 1
SECTIONS = [
    (Y_BACK, 0.0, 59.95, 56.5, 1.8, 2.4),
    (52.0, 0.6, 59.95, 56.5, 1.8, 2.4),
    (36.0, 1.1, 57.6, 56.4, 1.75, 2.25),
    (24.0, 1.5, 55.2, 56.3, 1.7, 2.15),
    (11.0, 1.8, 54.25, 56.0, 1.7, 2.1),
    (-80.0, 3.6, 49.0, 53.6, 1.6, 2.1),
]
N_FLARE = 5              # the first sections form the smoothly lofted flare

# slanted front cut: passes through crown point (FRONT_Y, FRONT_Z), leaning back going down
FRONT_Y = -70.1
FRONT_Z = 53.9
FRONT_SLOPE = 0.53       # dy/dz of the slanted front face
# lower front edge of the left leg
LEG_Y = -38.0
LEG_Z = 11.0
LEG_Z2 = 19.0            # where the leg edge meets the slanted face
NECK_Z = 31.6            # top of the clevis neck where it meets the slanted face

# vented box on top at the back
BOX_X = -2.1             # slight offset of the box
BOX_W = 72.0
BOX_FRONT_Y = 26.2
BOX_BACK_Y = 68.4        # box back face sits a little inside the shell rim
BOX_R = 7.0              # plan corner radius
BOX_TOP = 74.8
BOX_TOP_R = 100.0        # radius of the curved top (about Y)
BOX_FILLET = 5.0         # rounding of the top edges
BOX_WALL = 2.5
BOX_BASE_FILLET = 3.5      # blend between box and shell
WIN = 8.7                # square window size (front face)
WIN_HOLE = 4.3           # round hole diameter (back face)
WIN_ARC_R = 53.0
WIN_Z = 67.6             # centre of middle window
WIN_PITCH = 12.85        # window pitch along the arc (mm)
WIN_X = -4.1
WIN_ROT = 0.7            # fraction of the arc angle applied to the window rotation
N_WIN = 5

# holes on top of the shell (drilled normal to the surface)
SIDE_HOLE_D = 7.6
SIDE_HOLE_XC = 1.0
SIDE_HOLE_X = 29.5
SIDE_HOLE_Y = -8.7

# clevis tab at front right
CLV_X0 = 42.8
CLV_X1 = 63.0
CLV_H = 22.2
CLV_END_Y = -114.8
CLV_FORK_Y = -83.0
CLV_SLOT = 9.0
CLV_HOLE_D = 5.2
CLV_HOLE_Y = -98.4
CLV_FILLET = 2.5
SLIT_Y = -49.2           # thin relief slit between right wall and clevis neck
SLIT_H = 15.0

NPTS = 17


def section_at(y):
    """interpolated (xc, a, b, n_right, n_left) of the outer surface at station y"""
    if y >= SECTIONS[0][0]:
        return SECTIONS[0][1:]
    for s0, s1 in zip(SECTIONS[:-1], SECTIONS[1:]):
        if s1[0] <= y <= s0[0]:
            f = (s0[0] - y) / (s0[0] - s1[0])
            return tuple(p + f * (q - p) for p, q in zip(s0[1:], s1[1:]))
    return SECTIONS[-1][1:]


def wall_x(y, z, side=1, off=0.0):
    """x of the outer surface (offset inwards by off) at height z on the given side"""
    xc, a, b, nr, nl = section_at(y)
    n = nr if side > 0 else nl
    a, b = a - off, b - off
    u = max(0.0, 1.0 - (max(z, 0.0) / b) ** n)
    return xc + side * a * u ** (1.0 / n)


def arch_points(xc, a, b, nr, nl, y):
    """points of an asymmetric superellipse arch from (+a, 0) over the crown to (-a, 0)"""
    pts = []
    for i in range(NPTS):
        t = math.pi * i / (NPTS - 1)
        c, s = math.cos(t), math.sin(t)
        n = nr if c >= 0 else nl
        x = a * math.copysign(abs(c) ** (2.0 / n), c)
        z = b * abs(s) ** (2.0 / n)
        if i == 0:
            x, z = a, 0.0
        if i == NPTS - 1:
            x, z = -a, 0.0
        pts.append(cq.Vector(xc + x, y, z))
    return pts


def outer_wire(y, xc, a, b, nr, nl, off=0.0):
    pts = arch_points(xc, a - off, b - off, nr, nl, y)
    sp = cq.Edge.makeSpline(pts, tangents=[cq.Vector(0, 0, 1), cq.Vector(0, 0, -1)])
    return cq.Wire.assembleEdges([sp, cq.Edge.makeLine(pts[-1], pts[0])])


def inner_wire(y, xc, a, b, nr, nl, drop=6.0):
    pts = arch_points(xc, a - T, b - T, nr, nl, y)
    sp = cq.Edge.makeSpline(pts, tangents=[cq.Vector(0, 0, 1), cq.Vector(0, 0, -1)])
    p0, p1 = pts[0], pts[-1]
    q1 = cq.Vector(p1.x, y, -drop)
    q0 = cq.Vector(p0.x, y, -drop)
    return cq.Wire.assembleEdges([
        sp, cq.Edge.makeLine(p1, q1), cq.Edge.makeLine(q1, q0), cq.Edge.makeLine(q0, p0)])


def _loft(wires, ruled):
    return cq.Workplane("XY").add(cq.Solid.makeLoft(wires, ruled))


# ---------------- shell ----------------
flare_secs = SECTIONS[:N_FLARE]
front_secs = SECTIONS[N_FLARE - 1:]
outer = _loft([outer_wire(*s) for s in flare_secs], False).union(
    _loft([outer_wire(*s) for s in front_secs], True))

back_s = SECTIONS[0]
tip_s = SECTIONS[-1]
inner = (
    _loft([inner_wire(*s) for s in flare_secs], False)
    .union(_loft([inner_wire(*s) for s in front_secs]
                 + [inner_wire(tip_s[0] - 8.0, *tip_s[1:])], True))
    .union(_loft([inner_wire(*back_s), inner_wire(back_s[0] + 6.0, *back_s[1:])], True))
)



def y_cut(z):
    return FRONT_Y + FRONT_SLOPE * (FRONT_Z - z)


def yz_prism(pts, x0, x1):
    return cq.Workplane("YZ", origin=(x0, 0, 0)).polyline(pts).close().extrude(x1 - x0)


# slanted front face (right half keeps the wall down to the clevis neck)
cut_right = yz_prism([(-250.0, -20.0), (y_cut(NECK_Z), -20.0), (y_cut(NECK_Z), NECK_Z),
                      (y_cut(140.0), 140.0), (-250.0, 140.0)], 0.0, 150.0)
# left half: slanted face above LEG_Z2, stepped-back leg below
cut_left = yz_prism([(-250.0, -20.0), (LEG_Y, -20.0), (LEG_Y, LEG_Z),
                     (y_cut(LEG_Z2), LEG_Z2), (y_cut(140.0), 140.0),
                     (-250.0, 140.0)], -150.0, 0.0)
front_cut = cut_right.union(cut_left)
shell = outer.cut(front_cut).cut(inner)

# ---------------- vented box on top ----------------
box_l = BOX_BACK_Y - BOX_FRONT_Y
box_cy = 0.5 * (BOX_BACK_Y + BOX_FRONT_Y)
box_outer = (
    cq.Workplane("XY", origin=(BOX_X, box_cy, 10))
    .rect(BOX_W, box_l).extrude(80)
    .edges("|Z").fillet(BOX_R)
)
top_cyl = (
    cq.Workplane("XZ", origin=(BOX_X, Y_BACK + 5, BOX_TOP - BOX_TOP_R))
    .circle(BOX_TOP_R).extrude(box_l + 20)
)
box_outer = box_outer.intersect(top_cyl)
box_outer = box_outer.faces(">Z").edges().fillet(BOX_FILLET)

box_cav = (
    cq.Workplane("XY", origin=(BOX_X, box_cy, 10))
    .rect(BOX_W - 2 * BOX_WALL, box_l - 2 * BOX_WALL).extrude(80)
    .edges("|Z").fillet(BOX_R - BOX_WALL)
)
cav_cyl = (
    cq.Workplane("XZ", origin=(BOX_X, Y_BACK + 5, BOX_TOP - BOX_TOP_R))
    .circle(BOX_TOP_R - BOX_WALL).extrude(box_l + 20)
)
box_cav = box_cav.intersect(cav_cyl)

box_solid = box_outer.cut(outer)
box_cav = box_cav.cut(outer)

body = shell.union(box_solid)
# concave fillet where the box meets the shell
junction = [
    e for e in body.edges().vals()
    if (lambda bb: bb.zmin > 30 and bb.zmax < 60
        and bb.ymin > BOX_FRONT_Y - 1 and bb.ymax < BOX_BACK_Y + 1
        and bb.xmin > BOX_X - BOX_W / 2 - 1 and bb.xmax < BOX_X + BOX_W / 2 + 1)(e.BoundingBox())
]
body = body.newObject(junction).fillet(BOX_BASE_FILLET)
body = body.cut(box_cav)

# square windows in the front face, round holes in the back face
arc_cz = WIN_Z - WIN_ARC_R
for i in range(N_WIN):
    ang = (i - (N_WIN - 1) / 2.0) * math.degrees(WIN_PITCH / WIN_ARC_R)
    r = math.radians(ang)
    cx = WIN_X + WIN_ARC_R * math.sin(r)
    cz = arc_cz + WIN_ARC_R * math.cos(r)
    win = (
        cq.Workplane("XZ", origin=(0, BOX_FRONT_Y + 6, 0))
        .center(cx, cz)
        .transformed(rotate=(0, 0, WIN_ROT * ang))
        .rect(WIN, WIN).extrude(12)
    )
    body = body.cut(win)
    hole = (
        cq.Workplane("XZ", origin=(0, BOX_BACK_Y + 2, 0))
        .center(cx, cz)
        .circle(WIN_HOLE / 2.0).extrude(8)
    )
    body = body.cut(hole)

# ---------------- holes on top (drilled normal to the surface) ----------------
for sx in (-1, 1):
    xc, a_h, b_h, nr_h, nl_h = section_at(SIDE_HOLE_Y)
    n_h = nr_h if sx > 0 else nl_h
    px = SIDE_HOLE_XC + sx * SIDE_HOLE_X
    xr = abs(px - xc)
    pz = b_h * max(0.0, 1.0 - (xr / a_h) ** n_h) ** (1.0 / n_h)
    gx = n_h * xr ** (n_h - 1) / a_h ** n_h
    gz = n_h * pz ** (n_h - 1) / b_h ** n_h
    gl = math.hypot(gx, gz)
    gx, gz = sx * gx / gl, gz / gl
    h = cq.Solid.makeCylinder(
        SIDE_HOLE_D / 2.0, 30,
        cq.Vector(px - gx * 15, SIDE_HOLE_Y, pz - gz * 15),
        cq.Vector(gx, 0, gz),
    )
    body = body.cut(cq.Workplane("XY").add(h))


# ---------------- clevis tab with its neck ----------------
def neck_wire(y, pts):
    return cq.Wire.makePolygon([cq.Vector(x, y, z) for (x, z) in pts], close=True)


def wall_section(y, z_top, inset=0.6):
    """neck section hidden just inside the right wall (plus some material inwards)"""
    return [(wall_x(y, 0.0, 1, T + 2.0), 0.0), (wall_x(y, 0.0, 1, inset), 0.0),
            (wall_x(y, 12.0, 1, inset), 12.0), (wall_x(y, z_top - 3.0, 1, inset), z_top - 3.0),
            (wall_x(y, z_top, 1, inset), z_top)]


y_nk = y_cut(NECK_Z)
NECK_SECS = [
    (-50.0, wall_section(-50.0, 31.5, 0.2)),
    (y_nk, [(40.0, 0.0), (wall_x(y_nk, 0.0, 1, 0.0) + 0.8, 0.0),
            (52.5, 20.0), (wall_x(y_nk, NECK_Z, 1, 0.3), NECK_Z),
            (wall_x(y_nk, NECK_Z, 1, T + 0.5), NECK_Z)]),
    (-70.4, [(41.5, 0.0), (58.3, 0.0), (52.5, 24.5), (44.0, 29.4), (41.5, 29.4)]),
    (-78.2, [(42.3, 0.0), (61.0, 0.0), (58.0, 22.8), (47.0, 26.3), (42.3, 26.3)]),
    (CLV_FORK_Y - 1.0, [(CLV_X0, 0.0), (CLV_X1, 0.0), (CLV_X1, CLV_H - 1.2),
                        (CLV_X0 + 9.0, CLV_H + 0.3), (CLV_X0, CLV_H + 0.3)]),
]
neck = cq.Workplane("XY").add(
    cq.Solid.makeLoft([neck_wire(y, p) for (y, p) in NECK_SECS], False))
# keep the rear part of the neck inside the wall skin so it blends without bumps
NECK_CLIP_Y = -54.0
skin_in = _loft([outer_wire(*s, off=0.3) for s in front_secs], True)
neck_clip = cq.Workplane("XY").box(100, 40, 80, centered=(False, False, True)).translate(
    (0, NECK_CLIP_Y, 20)).cut(skin_in)
neck = neck.cut(neck_clip)

end_r = CLV_H / 2.0
end_cy = CLV_END_Y + end_r
prongs = (
    cq.Workplane("YZ", origin=(CLV_X0, 0, 0))
    .moveTo(CLV_FORK_Y, 0)
    .lineTo(end_cy, 0)
    .threePointArc((CLV_END_Y, end_r), (end_cy, CLV_H))
    .lineTo(CLV_FORK_Y, CLV_H)
    .close()
    .extrude(CLV_X1 - CLV_X0)
)
prongs = prongs.faces("<X or >X").edges(
    cq.selectors.BoxSelector((0, CLV_END_Y - 10, -10), (100, CLV_FORK_Y - 0.5, 50))
).fillet(CLV_FILLET)

clevis = prongs.union(neck)
body = body.union(clevis)

# clean the inside of the shell behind the clevis neck
inner_trim = inner.intersect(
    cq.Workplane("XY").box(200, 200, 200, centered=(True, False, True)).translate((0, -50.5, 0)))
body = body.cut(inner_trim)

# fork slot, cross pin hole and the relief slit
slot_cx = (CLV_X0 + CLV_X1) / 2.0
slot = cq.Workplane("XY").box(CLV_SLOT, 50, 40).translate((slot_cx, CLV_FORK_Y - 25, 15))
body = body.cut(slot)
pin = cq.Solid.makeCylinder(CLV_HOLE_D / 2.0, 40, cq.Vector(30, CLV_HOLE_Y, end_r),
                            cq.Vector(1, 0, 0))
body = body.cut(cq.Workplane("XY").add(pin))

slit = cq.Workplane("XY").box(20, 0.8, SLIT_H + 1).translate((52, SLIT_Y, (SLIT_H - 1) / 2.0))
body = body.cut(slit)

result = body
